import cadquery as cq
import math

# =====================================================================
#  Open box body (open-top wagon / container body) with gable end walls,
#  side stanchions, diagonal braces, double side doors and a top-hung
#  end door on the +X end.  Units: mm.
# =====================================================================

# ---------------- driving dimensions ----------------
POST_PITCH = 933.0           # pitch of the side-wall stanchions
DOOR_PITCH = 1264.0          # centre distance of the two side-door posts
HALF_DOOR = DOOR_PITCH / 2.0
POST_XS = [HALF_DOOR + i * POST_PITCH for i in range(4)]   # 632 .. 3431
X_END = POST_XS[-1]          # corner post centre (+/-)
POST_W = 85.0                # stanchion width (X)
POST_D = 65.0                # stanchion depth (Y) beyond the sheet
CORNER_W = 100.0             # corner post width (X)
POST_R = 14.0                # rounding of the stanchion outer edges

Y_PL_IN = 995.0              # inner face of side-wall sheet
PL_T = 30.0                  # sheet thickness
Y_PL_OUT = Y_PL_IN + PL_T
Y_OUT = 1118.0               # outer face of stanchions / gable width
Z_WALL_BOT = 205.0           # bottom edge of the side-wall sheet
BOT_ANGLE_H = 16.0           # bottom edge angle height
DOUBLER_T = 4.0              # diagonal doubler sheet thickness
Z_RAIL_BOT = 1440.0          # underside of top rail
Z_RAIL_TOP = 1570.0          # top of top rail
Y_RAIL_IN = 980.0
Y_RAIL_OUT = 1185.0

# gable (both ends)
Z_SHOULDER = 1664.0
Z_APEX = 1995.0
HALF_FLAT = 149.0
END_POST_Y = 422.0
GABLE_INSET = 58.0          # door-end gable is inset from the fixed-end gable

# side door
DOOR_LEAF_D = 50.0           # leaf depth
Z_SILL_BOT = 115.0

# end door (+X end)
DOOR_HALF_W = 1040.0
Z_EDOOR_BOT = 240.0
Z_EDOOR_PANEL_TOP = 1320.0
TUBE_R = 56.0
TUBE_Z = 1500.0
TUBE_OFF = 95.0              # hinge tube axis outboard of the corner posts
EDOOR_STIFF_Y = (-924.0, -299.0, 299.0, 924.0)   # vertical stiffeners of the end door
EDOOR_STIFF_W = 86.0
EDOOR_FRAME_D = 82.0         # depth of the end-door framing from the corner-post face


# ---------------- helpers ----------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def polyhedron(verts, faces):
    fs = []
    for f in faces:
        pts = [cq.Vector(*verts[i]) for i in f]
        fs.append(cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True)))
    so = cq.Solid.makeSolid(cq.Shell.makeShell(fs))
    if so.Volume() < 0:
        so = cq.Solid(so.wrapped.Reversed())
    return cq.Workplane("XY").add(so)


def gable_pts(zb):
    return [(-Y_OUT, zb), (Y_OUT, zb), (Y_OUT, Z_SHOULDER),
            (HALF_FLAT, Z_APEX), (-HALF_FLAT, Z_APEX), (-Y_OUT, Z_SHOULDER)]


def yz_prism(pts, x0, x1):
    """polygon in the YZ plane extruded along +X from x0 to x1"""
    return cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close().extrude(x1 - x0)


def xz_prism(pts, y0, y1):
    """polygon (x, z) extruded along Y from y0 to y1"""
    return (cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
            .extrude(y1 - y0))


def offset_poly(pts, d):
    """inward offset of a convex CCW polygon (y, z) by d"""
    n = len(pts)
    lines = []
    for i in range(n):
        (y0, z0), (y1, z1) = pts[i], pts[(i + 1) % n]
        dy, dz = y1 - y0, z1 - z0
        ln = math.hypot(dy, dz)
        ny, nz = -dz / ln, dy / ln
        lines.append(((y0 + ny * d, z0 + nz * d), (dy, dz)))
    out = []
    for i in range(n):
        (p, r), (q, s) = lines[i - 1], lines[i]
        den = r[0] * s[1] - r[1] * s[0]
        t = ((q[0] - p[0]) * s[1] - (q[1] - p[1]) * s[0]) / den
        out.append((p[0] + t * r[0], p[1] + t * r[1]))
    return out


def gable_band(d0, d1, x0, x1, zmin):
    """strip between inward offsets d0 and d1 of the gable outline, above zmin"""
    base = gable_pts(zmin - 400.0)
    p0 = base if d0 <= 0 else offset_poly(base, d0)
    p1 = offset_poly(base, d1)
    band = yz_prism(p0, x0, x1).cut(yz_prism(p1, x0 - 1, x1 + 1))
    return band.intersect(box(x0 - 2, x1 + 2, -Y_OUT - 5, Y_OUT + 5, zmin, Z_APEX + 5))


def gable_plate(d, x0, x1, zmin):
    """gable outline offset inward by d, extruded x0..x1, cut off below zmin"""
    base = gable_pts(zmin - 400.0)
    p = base if d <= 0 else offset_poly(base, d)
    return yz_prism(p, x0, x1).intersect(box(x0 - 2, x1 + 2, -Y_OUT - 5, Y_OUT + 5, zmin, Z_APEX + 5))


def v_pocket(xc, zc, w, h, y_face, depth, a=90.0, e=110.0, b=200.0, c=245.0):
    """pressed-panel pocket (cut from the outer face at y_face toward -Y):
    rectangular mouth, smaller floor with a V-notch at its top edge.
    a: side inset, e: bottom inset, b/c: top inset at the floor corners / V apex"""
    yi = y_face - depth
    V = [(xc - w / 2, y_face + 1, zc - h / 2), (xc + w / 2, y_face + 1, zc - h / 2),
         (xc + w / 2, y_face + 1, zc + h / 2), (xc - w / 2, y_face + 1, zc + h / 2),
         (xc - w / 2 + a, yi, zc - h / 2 + e), (xc + w / 2 - a, yi, zc - h / 2 + e),
         (xc + w / 2 - a, yi, zc + h / 2 - b), (xc, yi, zc + h / 2 - c),
         (xc - w / 2 + a, yi, zc + h / 2 - b)]
    F = [(0, 1, 2, 3), (0, 4, 5, 1), (1, 5, 6, 2), (3, 2, 7), (2, 6, 7), (3, 7, 8),
         (0, 3, 8, 4), (4, 8, 7, 6, 5)]
    return polyhedron(V, F)


def ycyl(x, z, r, y0, y1):
    return cq.Workplane("XZ", origin=(x, y1, z)).circle(r).extrude(y1 - y0)


def zcyl(x, y, r, z0, z1):
    return cq.Workplane("XY", origin=(x, y, z0)).circle(r).extrude(z1 - z0)


# ---------------- one side wall (+Y side), mirrored later ----------------
def side_wall():
    xa, xb = -X_END - CORNER_W / 2, X_END + CORNER_W / 2
    w = box(xa, xb, Y_PL_IN, Y_PL_OUT, Z_WALL_BOT, Z_RAIL_BOT)
    # stanchions (incl. corner posts) down to the ground
    for sx in (-1, 1):
        for i, px in enumerate(POST_XS):
            corner = (i == len(POST_XS) - 1)
            pw = CORNER_W if corner else POST_W
            yo_ = Y_OUT if corner else Y_PL_OUT + POST_D
            p = box(sx * px - pw / 2, sx * px + pw / 2, Y_PL_OUT, yo_, 0, Z_RAIL_BOT)
            p = p.edges("|Z and >Y").fillet(POST_R)
            w = w.union(p)
    # diagonal brace lines in the four panels next to the door, rising towards +X:
    # the lower triangle of each of these panels carries a thin doubler sheet,
    # so the panel shows a single diagonal edge
    for (pa, pb) in [(-POST_XS[2], -POST_XS[1]), (-POST_XS[1], -POST_XS[0]),
                     (POST_XS[0], POST_XS[1]), (POST_XS[1], POST_XS[2])]:
        x0 = pa + POST_W / 2
        x1 = pb - POST_W / 2
        z0, z1 = Z_WALL_BOT + BOT_ANGLE_H, Z_RAIL_BOT
        tri = xz_prism([(x0, z0), (x1, z0), (x1, z1)], Y_PL_OUT - 1, Y_PL_OUT + DOUBLER_T)
        w = w.union(tri)
    # bottom edge angle
    for (p0, p1) in [(xa, -HALF_DOOR), (HALF_DOOR, xb)]:
        w = w.union(box(p0, p1, Y_PL_OUT, Y_PL_OUT + 35, Z_WALL_BOT, Z_WALL_BOT + BOT_ANGLE_H))
    # top rail: box section with a guide rib and channel on top, stepped outer face
    xr0, xr1 = xa - 5, xb + 5
    rail = box(xr0, xr1, Y_RAIL_IN, Y_RAIL_OUT, Z_RAIL_BOT, Z_RAIL_TOP)
    rail = rail.cut(box(xr0 - 1, xr1 + 1, Y_RAIL_OUT - 30, Y_RAIL_OUT + 1,
                        Z_RAIL_TOP - 36, Z_RAIL_TOP + 1))          # top outer notch
    rail = rail.cut(box(xr0 - 1, xr1 + 1, Y_RAIL_OUT - 8, Y_RAIL_OUT + 1,
                        Z_RAIL_BOT - 1, Z_RAIL_BOT + 47))          # recessed lower lip
    rail = rail.cut(box(xr0 - 1, xr1 + 1, Y_RAIL_IN + 70, Y_RAIL_IN + 110,
                        Z_RAIL_TOP - 14, Z_RAIL_TOP + 1))
    rail = rail.union(box(xr0, xr1, Y_RAIL_IN + 20, Y_RAIL_IN + 50,
                          Z_RAIL_TOP, Z_RAIL_TOP + 18))
    w = w.union(rail)

    # ---- double side door (on the outside of the sheet) ----
    dx0, dx1 = -HALF_DOOR + POST_W / 2, HALF_DOOR - POST_W / 2
    yo = Y_PL_OUT + DOOR_LEAF_D
    # door head and sill frame
    w = w.union(box(dx0, dx1, Y_PL_OUT, yo + 5, Z_RAIL_BOT - 45, Z_RAIL_BOT))
    sill = box(-HALF_DOOR - POST_W / 2, HALF_DOOR + POST_W / 2,
               Y_PL_IN, yo + 5, Z_SILL_BOT, Z_WALL_BOT + 10)
    sill = sill.cut(box(-HALF_DOOR + POST_W / 2, HALF_DOOR - POST_W / 2,
                        Y_PL_IN + 14, yo - 9, Z_SILL_BOT - 1, Z_WALL_BOT - 20))
    w = w.union(sill)
    gap = 8.0
    zl0, zl1 = Z_WALL_BOT + 20, Z_RAIL_BOT - 55
    for sx in (-1, 1):
        lx0, lx1 = (dx0 + 8, -gap) if sx < 0 else (gap, dx1 - 8)
        leaf = box(lx0, lx1, Y_PL_OUT, yo, zl0, zl1)
        inset = 35.0
        pw, ph = (lx1 - lx0) - 2 * inset, (zl1 - zl0) - 2 * inset
        leaf = leaf.cut(v_pocket((lx0 + lx1) / 2, (zl0 + zl1) / 2, pw, ph, yo, 42.0))
        w = w.union(leaf)
        # hinges on the outer edges
        hx = sx * (dx1 + 2)
        for hz in (zl0 + 110, zl1 - 170):
            w = w.union(zcyl(hx, yo + 18, 17, hz, hz + 110))
            hb0, hb1 = (hx - 110, hx) if sx > 0 else (hx, hx + 110)
            w = w.union(box(hb0, hb1, yo - 2, yo + 12, hz + 25, hz + 85))
    # central locking bar with guides and lever
    w = w.union(zcyl(0, yo + 28, 24, Z_SILL_BOT + 40, zl1 + 20))
    for gz in (300, 660, 1020):
        w = w.union(box(-34, 34, yo - 2, yo + 44, gz, gz + 70))
    w = w.union(box(-14, 14, yo + 40, yo + 50, 760, 980))       # operating handle
    lev = (cq.Workplane("XY").box(300, 22, 34)
           .rotate((0, 0, 0), (0, 1, 0), 16)
           .translate((135, yo + 30, 300)))
    w = w.union(lev)
    w = w.union(box(200, 300, yo - 2, yo + 20, 230, 300))
    return w


wall_p = side_wall()
result = wall_p.union(wall_p.mirror("XZ"))

# ---------------- fixed end wall with gable (-X end) ----------------
XE = -X_END - CORNER_W / 2          # outer face of corner posts (-X)
result = result.union(yz_prism(gable_pts(Z_WALL_BOT), XE - 22, XE + 1))
result = result.union(gable_band(0, 55.0, XE - 45, XE - 21, Z_RAIL_TOP))
gable_env = yz_prism(gable_pts(-10.0), XE - 200, XE + 10)
for sy in (-1, 1):
    yc = sy * END_POST_Y
    post = box(XE - 90, XE - 21, yc - 40, yc + 40, 0, Z_APEX)
    result = result.union(post.intersect(gable_env))

# ---------------- door end (+X end) ----------------
XD = X_END + CORNER_W / 2           # outer face of corner posts (+X)
zg = TUBE_Z + TUBE_R - 15
result = result.union(gable_plate(GABLE_INSET, XD - 1, XD + 20, Z_RAIL_BOT))
result = result.union(gable_band(GABLE_INSET, GABLE_INSET + 50.0, XD + 19, XD + 64, zg))
for sy in (-1, 1):
    yc = sy * END_POST_Y
    post = box(XD + 19, XD + 55, yc - 35, yc + 35, zg - 20, Z_APEX)
    result = result.union(post.intersect(gable_plate(GABLE_INSET + 49.0, XD, XD + 70, zg - 20)))
# hinge tube
TX = XD + TUBE_OFF
result = result.union(ycyl(TX, TUBE_Z, TUBE_R, -Y_OUT + 20, Y_OUT - 20))
# hinge lugs, pins and brackets at the rail ends
for sy in (-1, 1):
    y0, y1 = (Y_OUT - 22, Y_OUT + 8) if sy > 0 else (-Y_OUT - 8, -Y_OUT + 22)
    lug = ycyl(TX, TUBE_Z, TUBE_R + 12, y0, y1)
    lug = lug.union(xz_prism([(XD - 40, TUBE_Z - 42), (TX, TUBE_Z - TUBE_R - 12),
                              (TX, TUBE_Z + TUBE_R + 12), (XD - 40, TUBE_Z + 42)], y0, y1))
    result = result.union(lug)
    result = result.union(ycyl(XD - 20, TUBE_Z, 24, y0 - 6, y1 + 6))
    yb0, yb1 = (Y_OUT - 45, Y_OUT) if sy > 0 else (-Y_OUT, -Y_OUT + 45)
    result = result.union(box(XD - 30, XD + 15, yb0, yb1, 1320, Z_RAIL_BOT))
# door leaf: recessed sheet, stiles, stiffeners, bottom rail
XP = XD + 16
XF = XD + EDOOR_FRAME_D              # outer plane of the door framing
result = result.union(box(XD - 1, XP + 15, -DOOR_HALF_W, DOOR_HALF_W, Z_EDOOR_BOT, Z_EDOOR_PANEL_TOP))
for yc in EDOOR_STIFF_Y:
    result = result.union(box(XP + 15, XF, yc - EDOOR_STIFF_W / 2, yc + EDOOR_STIFF_W / 2,
                              Z_EDOOR_BOT, Z_EDOOR_PANEL_TOP))
result = result.union(box(XP + 15, XF, -DOOR_HALF_W, DOOR_HALF_W, Z_EDOOR_BOT, Z_EDOOR_BOT + 35))
# top apron of the door between panel and hinge tube: trapezoid in the end
# view (full width at the tube, as wide as the framing at the bottom)
APRON_HW = Y_OUT - 10.0
apron = xz_prism([(XD - 1, Z_EDOOR_PANEL_TOP), (XF, Z_EDOOR_PANEL_TOP),
                  (XF + 8, TUBE_Z - 25), (TX, TUBE_Z), (XD - 1, TUBE_Z)],
                 -APRON_HW, APRON_HW)
ch_y, ch_z = APRON_HW - (abs(EDOOR_STIFF_Y[0]) + EDOOR_STIFF_W / 2 - 2), 165.0
cutter = yz_prism([(-APRON_HW - 10, Z_EDOOR_PANEL_TOP - 1),
                   (-APRON_HW + ch_y, Z_EDOOR_PANEL_TOP - 1),
                   (-APRON_HW - 10, Z_EDOOR_PANEL_TOP + ch_z * (ch_y + 10) / ch_y)],
                  XD - 5, TX + 80)
apron = apron.cut(cutter).cut(cutter.mirror("XZ"))
result = result.union(apron)

VIEW = {"azimuth": 45, "elevation": 26}
